import math
import cadquery as cq

# =====================================================================
#  Turned/moulded funnel-cup adapter
#  axis of revolution = Y ; the open cup faces -Y, the pipe stub +Y,
#  the radial side port enters the rear boss from +Z.
# =====================================================================

# ---------------- outer steps (mm) ----------------
R_FLANGE = 59.0      # big flange outer radius
L_FLANGE = 29.7      # flange axial length
R_GROOVE = 55.0      # outer radius of the deep annular groove in the flange front
GROOVE_DEPTH = 26.0  # depth of that groove into the flange
R_CUP = 48.4         # front cup outer radius
L_CUP = 25.5         # cup protrusion in front of the flange face
CUP_RIM = 0.5        # wall thickness at the knife-edge rim of the cup
R_REAR = 42.0        # rear boss radius
L_REAR = 21.4        # rear boss length
R_PIPE = 12.35       # pipe stub outer radius
L_PIPE = 21.2        # pipe stub length
PIPE_WALL = 0.5      # thin pipe stub wall

# ---------------- inner funnel bowl ----------------
CONE_END_R = 44.0    # drafted (conical) inner wall ends at this radius ...
CONE_END_Y = 0.0     # ... in the plane of the flange front face
BOWL_RADIUS = 27.0   # concave arc, tangent to the cone, running down to a flat floor
HOLE_ROUND = 6.5     # convex round from the flat floor into the bore
R_BORE = 8.5         # central through bore radius

# ---------------- radial side port (from +Z) ----------------
SIDE_HOLE_D = 17.0
SIDE_HOLE_OFFSET = 8.75  # centre distance behind the flange back face
SIDE_HOLE_BELOW = 2.0    # drilled this far past the bottom of the bore

# ---------------- derived ----------------
y_rim = -L_CUP
y_fl_front = 0.0
y_fl_back = L_FLANGE
y_rear_back = L_FLANGE + L_REAR
y_pipe_end = y_rear_back + L_PIPE
R_RIM_IN = R_CUP - CUP_RIM
R_PIPE_IN = R_PIPE - PIPE_WALL
y_side = y_fl_back + SIDE_HOLE_OFFSET
y_pipe_bore = y_side + SIDE_HOLE_D / 2 + 2.0   # larger pipe bore starts behind the port

# dished floor: arc tangent to the drafted cone, ending horizontal at the floor
tx, ty = CONE_END_R - R_RIM_IN, CONE_END_Y - y_rim
tl = math.hypot(tx, ty)
nx, ny = -ty / tl, tx / tl                      # inward normal of the cone line
arc_c = (CONE_END_R + BOWL_RADIUS * nx, CONE_END_Y + BOWL_RADIUS * ny)
a0 = math.atan2(CONE_END_Y - arc_c[1], CONE_END_R - arc_c[0])
am = 0.5 * (a0 + math.pi / 2.0)
arc_mid = (arc_c[0] + BOWL_RADIUS * math.cos(am), arc_c[1] + BOWL_RADIUS * math.sin(am))
floor_pt = (arc_c[0], arc_c[1] + BOWL_RADIUS)   # horizontal tangent point
y_floor = floor_pt[1]

# convex round from the floor into the bore
rr = HOLE_ROUND
kk = rr * (1.0 - 1.0 / math.sqrt(2.0))
y_bore_start = y_floor + rr


def revolve_y(wp):
    return wp.revolve(360, (0, 0, 0), (0, 1, 0))


# ---------------- outer body (profile: X = radius, Y = axial) ----------------
outer = revolve_y(
    cq.Workplane("XY")
    .moveTo(0, y_rim)
    .lineTo(R_CUP, y_rim)
    .lineTo(R_CUP, y_fl_front + GROOVE_DEPTH)
    .lineTo(R_GROOVE, y_fl_front + GROOVE_DEPTH)
    .lineTo(R_GROOVE, y_fl_front)
    .lineTo(R_FLANGE, y_fl_front)
    .lineTo(R_FLANGE, y_fl_back)
    .lineTo(R_REAR, y_fl_back)
    .lineTo(R_REAR, y_rear_back)
    .lineTo(R_PIPE, y_rear_back)
    .lineTo(R_PIPE, y_pipe_end)
    .lineTo(0, y_pipe_end)
    .close()
)
# turn the cylinder seams to the lower back side
outer = outer.rotate((0, 0, 0), (0, 1, 0), 130)

# ---------------- inner cavity: cone + dished floor + round + bores ----------------
e = 1.0  # overshoot past the open ends
cavity = revolve_y(
    cq.Workplane("XY")
    .moveTo(0, y_rim - e)
    .lineTo(R_RIM_IN, y_rim - e)
    .lineTo(R_RIM_IN, y_rim)
    .lineTo(CONE_END_R, CONE_END_Y)                                 # drafted wall
    .threePointArc(arc_mid, floor_pt)                               # dished floor
    .lineTo(R_BORE + rr, y_floor)                                   # flat floor
    .threePointArc((R_BORE + kk, y_floor + kk), (R_BORE, y_bore_start))  # round
    .lineTo(R_BORE, y_pipe_bore)                                    # through bore
    .lineTo(R_PIPE_IN, y_pipe_bore)
    .lineTo(R_PIPE_IN, y_pipe_end + e)                              # pipe bore
    .lineTo(0, y_pipe_end + e)
    .close()
)
# cavity seam toward the upper right (behind the rim in the main view)
cavity = cavity.rotate((0, 0, 0), (0, 1, 0), -45)

body = outer.cut(cavity)

# ---------------- radial side port, drilled from the top through the bore ----------------
side = (
    cq.Workplane("XY", origin=(0, y_side, -R_BORE - SIDE_HOLE_BELOW))
    .circle(SIDE_HOLE_D / 2)
    .extrude(R_REAR + R_BORE + SIDE_HOLE_BELOW + 5)
    .rotate((0, y_side, 0), (0, y_side, 1), 180)   # seam of the port wall to -X
)
body = body.cut(side)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
